import math
import cadquery as cq

# =====================================================================
#  Wedge-topped holder block
#  X = width, Y = depth (flat front face at Y = 0), Z = height
# =====================================================================

# ---------------- main body (mm) ----------------
W = 52.4              # width along X
H = 50.0              # overall height
D_BOT = 21.65         # depth of the lower, vertical-backed part
D_TIP = 28.85         # depth at the tip of the sloped top
SLOPE = 30.0          # sloped top face, degrees from horizontal
R_FRONT_TOP = 3.5     # round between front face and sloped top
R_FRONT_BOT = 2.0     # round on the front / bottom edge
R_BEND = 7.5          # concave round between the rear neck and the back wall
R_BACK_CORNER = 4.5   # rounds on the rear side edges

# ---------------- pocket in the sloped face ----------------
# local slope coordinates: u = X, s = distance down the slope from the
# front crease line, depth measured perpendicular into the sloped face
POCKET_HALF_W = 25.0
POCKET_S0 = 7.2
POCKET_S1 = 32.1
POCKET_DEPTH = 5.2
POCKET_R = 3.5            # corner radius of the pocket outline
POCKET_FLOOR_R = 1.0      # round between pocket floor and walls
BAND_HALF_W = 10.0        # raised centre band
BAND_DEPTH = 3.1          # band top below the sloped face
CIRCLE_D = 19.0           # round recess in the band
CIRCLE_S = 20.0
CIRCLE_DEPTH = 2.3
NOTCH_ANG = -39.0         # key notch leaving the round recess
NOTCH_R0 = 9.0
NOTCH_R1 = 16.2
NOTCH_W = 2.3
NOTCH_DEPTH = 7.5
DHOLE_X = 16.0            # two D-shaped holes in the side floors
DHOLE_S = 24.6
DHOLE_R = 3.2
DHOLE_FLAT = 2.9
DHOLE_DEPTH = 10.0

# ---------------- vertical slot in the front face ----------------
SLOT_W = 9.4
SLOT_Z0, SLOT_Z1 = 8.1, 39.6       # opening on the front face
SLOT_IZ0, SLOT_IZ1 = 13.0, 26.8    # level deep part
SLOT_T = 20.0                      # depth of the deep part
SLOT_STEP = 10.0                   # depth of the lower step

# ---------------- horizontal slot in the rear neck ----------------
NSLOT_LEN = 37.6
NSLOT_W = 5.0
NSLOT_POS = 9.0        # centre distance from the tip edge, down the neck
NSLOT_DEPTH = 3.0

# ---------------- small slot in the bottom ----------------
BSLOT_L = 4.5
BSLOT_W = 3.0
BSLOT_R = 1.0
BSLOT_X = 12.2
BSLOT_Y = 4.6
BSLOT_DEPTH = 5.0

# ---------------- derived geometry ----------------
a = math.radians(SLOPE)
ta, sa, ca = math.tan(a), math.sin(a), math.cos(a)
# height where the sloped face line meets the front plane (sharp crease),
# chosen so that the rounded crease tops out at H
half = math.radians((90.0 - SLOPE) / 2.0)
bis = cq.Vector(ca, -1.0 - sa, 0).normalized()
Z_S0 = H - (bis.y * R_FRONT_TOP / math.sin(half) + R_FRONT_TOP)
Z_TIP = Z_S0 - ta * D_TIP
Z_NECK = Z_TIP - (D_TIP - D_BOT) / ta    # neck is perpendicular to the slope

# ---------------- main body ----------------
body = (
    cq.Workplane("YZ", origin=(-W / 2, 0, 0))
    .polyline([(0, 0), (D_BOT, 0), (D_BOT, Z_NECK), (D_TIP, Z_TIP), (0, Z_S0)])
    .close()
    .extrude(W)
)
body = body.edges(cq.selectors.NearestToPointSelector((0, 0, Z_S0))).fillet(R_FRONT_TOP)
body = body.edges(cq.selectors.NearestToPointSelector((0, D_BOT, Z_NECK))).fillet(R_BEND)
body = body.edges(cq.selectors.NearestToPointSelector((0, 0, 0))).fillet(R_FRONT_BOT)


def rear_side_edges(wp):
    """Edges of the two side faces along the back wall, bend and neck."""
    sel = []
    for e in wp.edges().vals():
        bb = e.BoundingBox()
        if abs(bb.xmax - bb.xmin) < 1e-3 and abs(abs(bb.xmin) - W / 2) < 1e-3:
            c = e.Center()
            if c.y > D_BOT - 5 and c.z < Z_TIP - 0.5:
                sel.append(e)
    return sel


body = body.newObject(rear_side_edges(body)).fillet(R_BACK_CORNER)

# ---------------- sloped face work frame ----------------
n_slope = cq.Vector(0, sa, ca)


def slope_wp(depth=0.0):
    """Workplane parallel to the sloped face, `depth` below it.
    Local x = X, local y points down the slope."""
    pl = cq.Plane(origin=cq.Vector(0, 0, Z_S0) - n_slope * depth,
                  xDir=(1, 0, 0), normal=n_slope)
    return cq.Workplane(pl)


# pocket with rounded corners and a rounded floor edge
pocket = (
    slope_wp(POCKET_DEPTH)
    .center(0, (POCKET_S0 + POCKET_S1) / 2)
    .rect(2 * POCKET_HALF_W, POCKET_S1 - POCKET_S0)
    .extrude(POCKET_DEPTH + 10)
    .edges(cq.selectors.ParallelDirSelector(n_slope)).fillet(POCKET_R)
    .faces(cq.selectors.DirectionMinMaxSelector(n_slope, directionMax=False))
    .edges().fillet(POCKET_FLOOR_R)
)
body = body.cut(pocket)

# raised centre band running the full length of the pocket
band = (
    slope_wp(POCKET_DEPTH + 0.5)
    .center(0, (POCKET_S0 + POCKET_S1) / 2)
    .rect(2 * BAND_HALF_W, POCKET_S1 - POCKET_S0 + 0.2)
    .extrude(POCKET_DEPTH + 0.5 - BAND_DEPTH)
)
body = body.union(band)

# round recess in the band
circ = (
    slope_wp(BAND_DEPTH + CIRCLE_DEPTH)
    .center(0, CIRCLE_S)
    .circle(CIRCLE_D / 2)
    .extrude(CIRCLE_DEPTH + 5)
)
body = body.cut(circ)

# key notch from the recess towards the front / +X side
ang = math.radians(NOTCH_ANG)
rmid = (NOTCH_R0 + NOTCH_R1) / 2
notch = (
    slope_wp(NOTCH_DEPTH)
    .center(rmid * math.cos(ang), CIRCLE_S + rmid * math.sin(ang))
    .transformed(rotate=(0, 0, NOTCH_ANG))
    .rect(NOTCH_R1 - NOTCH_R0, NOTCH_W)
    .extrude(NOTCH_DEPTH + 5)
)
body = body.cut(notch)

# D-shaped holes (flat side towards the centre)
for sx in (-1, 1):
    cx = sx * DHOLE_X
    rnd = (
        slope_wp(POCKET_DEPTH + DHOLE_DEPTH)
        .center(cx, DHOLE_S)
        .circle(DHOLE_R)
        .extrude(DHOLE_DEPTH + 1)
    )
    flat = (
        slope_wp(POCKET_DEPTH + DHOLE_DEPTH)
        .center(cx - sx * DHOLE_FLAT / 2, DHOLE_S)
        .rect(DHOLE_FLAT, 2 * DHOLE_R)
        .extrude(DHOLE_DEPTH + 1)
    )
    body = body.cut(rnd.union(flat))

# ---------------- front slot ----------------
def stadium_wire(zc, length, y):
    pl = cq.Plane(origin=(0, y, zc), xDir=(1, 0, 0), normal=(0, -1, 0))
    return cq.Workplane(pl).slot2D(length, SLOT_W, angle=90).wires().val()


def level_slot(z0, z1, depth):
    pl = cq.Plane(origin=(0, -0.5, (z0 + z1) / 2), xDir=(1, 0, 0), normal=(0, 1, 0))
    return cq.Workplane(pl).slot2D(z1 - z0, SLOT_W, angle=90).extrude(depth + 0.5)


# lower part: deep level slot plus a shorter one that leaves a step
slot_low = level_slot(SLOT_Z0, SLOT_IZ1, SLOT_STEP).union(level_slot(SLOT_IZ0, SLOT_IZ1, SLOT_T))
# upper part: roof descends from the top of the opening to the deep slot
slot_up = cq.Solid.makeLoft(
    [
        stadium_wire((SLOT_IZ0 + SLOT_Z1) / 2, SLOT_Z1 - SLOT_IZ0, 0.0),
        stadium_wire((SLOT_IZ0 + SLOT_IZ1) / 2, SLOT_IZ1 - SLOT_IZ0, SLOT_T),
    ],
    True,
)
body = body.cut(slot_low).cut(cq.Workplane().add(slot_up))

# ---------------- neck slot ----------------
neck_dir = cq.Vector(0, -sa, -ca)      # from the tip edge down the neck
n_neck = cq.Vector(0, ca, -sa)        # outward normal of the neck face
npt = cq.Vector(0, D_TIP, Z_TIP) + neck_dir * NSLOT_POS
nslot = (
    cq.Workplane(cq.Plane(origin=npt, xDir=(1, 0, 0), normal=n_neck))
    .slot2D(NSLOT_LEN, NSLOT_W)
    .extrude(-NSLOT_DEPTH)
)
body = body.cut(nslot)

# ---------------- bottom slot ----------------
bslot = (
    cq.Workplane("XY")
    .center(BSLOT_X, BSLOT_Y)
    .rect(BSLOT_L, BSLOT_W)
    .extrude(BSLOT_DEPTH)
    .edges("|Z").fillet(BSLOT_R)
)
body = body.cut(bslot)

result = body
